import math
import cadquery as cq

# =====================================================================
#  Half shell of a tapered handle / nozzle housing.
#  Split on (roughly) the XZ plane, open towards -Y, back wall at +Y.
#  Thin wall lofted through superellipse sections (straight side walls below
#  YS, superellipse back above); the inner skins are true offsets of the outer.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
T_WALL = 1.3          # shell wall thickness
Z_LOFT0 = -4.0        # lofts run a little past the finished part ...
Z_TOP = 146.0
Z_TRIM = 140.5        # ... and the outer skin is trimmed here
YF = -14.0            # front extension of the loft sections (trimmed by the split)

Z_BACK_TOP = 127.7    # top edge of the back wall
X_EAR_IN = 17.2       # the flat back wall top ends here, the ears rise beyond
EAR_TIP_Z = 139.7     # ear tip height
EAR_TIP_Y = -4.7

T_LIP = 3.9           # wall thickness along the lipped split edge
D_LIP = 2.0           # depth (Y) of the lip behind the split edge
Z_LIP_BOT = 21.0
Z_LIP_TOP_L = 90.0    # lip on the -X wall runs higher than on the +X wall
Z_LIP_TOP_R = 72.0
Z_NOTCH = 52.5        # V notch in both lips / step of the split line

HOLE_Z = 51.2         # screw hole in the back wall
HOLE_D = 7.8
BOSS_D = 11.6
BOSS_H = 1.9

BEAD_X = 15.9         # stiffening beads near the back corners
BEAD_Z0, BEAD_Z1 = 76.0, 120.5
BEAD_R = 4.0
BEAD_OUT = 0.8

EAR_PIN_Y, EAR_PIN_Z, EAR_PIN_R = -3.4, 131.0, 1.3
EAR_BOSS_R = 2.9      # D shaped pin boss on the inner face of the ears
EAR_PIN_H = 2.4       # pin boss height

# station table: z, half width a, back depth yb, superellipse exponent n,
# start of the curved back ys (straight side walls below)
Z_TAB = [0.0, 20.0, 40.0, 55.0, 70.0, 85.0, 100.0, 115.0, 127.0, 131.0, 135.0, 140.0, Z_TOP]
A_TAB = [28.2, 27.6, 26.2, 24.8, 23.2, 22.7, 22.5, 22.2, 21.7, 21.3, 20.1, 17.4, 13.0]
YB_TAB = [30.6, 29.6, 27.0, 23.0, 18.4, 14.2, 10.8, 9.5, 8.8, 8.7, 8.6, 8.5, 8.4]
N_TAB = [2.2, 2.2, 2.3, 2.35, 2.45, 2.55, 2.65, 2.8, 3.0, 3.1, 3.2, 3.3, 3.3]
YS_TAB = [0.0, 0.0, 0.0, 0.0, 0.0, 0.3, 0.8, 1.5, 2.2, 2.5, 2.8, 3.0, 3.0]

# split line seen from the side: (Y, z) points above the step at Z_NOTCH
FRONT_SPLINE = [(-1.8, 56.0), (-0.6, 71.0), (1.0, 86.0), (1.6, 95.0),
                (-1.0, 108.0), (-4.0, 123.0), (-5.0, 133.0), (-5.2, 150.0)]
# ear top seen from the side: from the tip backwards/down to the back wall
EAR_SPLINE = [(-1.5, 139.3), (2.1, 137.8), (5.1, 134.7), (7.7, 131.4),
              (9.7, 128.0), (10.8, 125.5)]


def interp(z, zs, vs):
    """monotone cubic (PCHIP) interpolation of a station table"""
    if z <= zs[0]:
        return vs[0]
    if z >= zs[-1]:
        return vs[-1]
    n = len(zs)
    h = [zs[i + 1] - zs[i] for i in range(n - 1)]
    d = [(vs[i + 1] - vs[i]) / h[i] for i in range(n - 1)]
    m = [0.0] * n
    m[0], m[-1] = d[0], d[-1]
    for i in range(1, n - 1):
        if d[i - 1] * d[i] <= 0:
            m[i] = 0.0
        else:
            w1 = 2 * h[i] + h[i - 1]
            w2 = h[i] + 2 * h[i - 1]
            m[i] = (w1 + w2) / (w1 / d[i - 1] + w2 / d[i])
    for i in range(n - 1):
        if zs[i] <= z <= zs[i + 1]:
            t = (z - zs[i]) / h[i]
            h00 = 2 * t ** 3 - 3 * t ** 2 + 1
            h10 = t ** 3 - 2 * t ** 2 + t
            h01 = -2 * t ** 3 + 3 * t ** 2
            h11 = t ** 3 - t ** 2
            return (h00 * vs[i] + h10 * h[i] * m[i] + h01 * vs[i + 1]
                    + h11 * h[i] * m[i + 1])
    return vs[-1]


def back_curve(z, inset=0.0, y0=-10.0, m=600):
    """dense polyline of one section: right side wall from y0, superellipse back,
    left side wall down to y0; offset inwards (true normal offset) by `inset`"""
    a = interp(z, Z_TAB, A_TAB)
    yb = interp(z, Z_TAB, YB_TAB)
    n = interp(z, Z_TAB, N_TAB)
    ys = interp(z, Z_TAB, YS_TAB)
    b = yb - ys
    e = 2.0 / n
    pts = [(a, y0), (a, ys - 0.5 * (ys - y0)), (a, ys)]
    for i in range(1, m):
        t = 0.5 * math.pi * i / m
        pts.append((a * math.cos(t) ** e, ys + b * math.sin(t) ** e))
    pts.append((0.0, yb))
    half = pts
    full = half + [(-p[0], p[1]) for p in reversed(half[:-1])]
    if inset == 0.0:
        return full
    out = []
    k = len(full)
    for i in range(k):
        p0 = full[max(i - 1, 0)]
        p1 = full[min(i + 1, k - 1)]
        tx, ty = p1[0] - p0[0], p1[1] - p0[1]
        ln = math.hypot(tx, ty)
        nx, ny = -ty / ln, tx / ln                     # left normal = inwards
        out.append((full[i][0] + inset * nx, full[i][1] + inset * ny))
    return out


def resample(poly, npts):
    """points evenly spaced along a polyline"""
    L = [0.0]
    for i in range(1, len(poly)):
        L.append(L[-1] + math.dist(poly[i], poly[i - 1]))
    tot = L[-1]
    res = []
    j = 0
    for k in range(npts):
        s = tot * k / (npts - 1)
        while j < len(L) - 2 and L[j + 1] < s:
            j += 1
        t = (s - L[j]) / max(L[j + 1] - L[j], 1e-12)
        res.append((poly[j][0] + t * (poly[j + 1][0] - poly[j][0]),
                    poly[j][1] + t * (poly[j + 1][1] - poly[j][1])))
    return res


def surf_y(x, z, inset=0.0):
    """Y of the back surface at (x, z)"""
    poly = back_curve(z, inset)
    best = None
    for i in range(len(poly) - 1):
        (x0, y0), (x1, y1) = poly[i], poly[i + 1]
        if (x0 - x) * (x1 - x) <= 0 and x0 != x1 and max(y0, y1) > 0:
            y = y0 + (x - x0) / (x1 - x0) * (y1 - y0)
            best = y if best is None else max(best, y)
    return best


def section_wire(z, inset=0.0, yf=YF, npts=25):
    poly = back_curve(z, inset)
    pts = [cq.Vector(p[0], p[1], z) for p in resample(poly, npts)]
    xr, xl, y0 = poly[0][0], poly[-1][0], poly[0][1]
    pts[0] = cq.Vector(xr, y0, z)
    pts[-1] = cq.Vector(xl, y0, z)
    edges = [
        cq.Edge.makeLine(cq.Vector(xl, yf, z), cq.Vector(xr, yf, z)),
        cq.Edge.makeLine(cq.Vector(xr, yf, z), cq.Vector(xr, y0, z)),
        cq.Edge.makeSpline(pts, tangents=[cq.Vector(0, 1, 0), cq.Vector(0, -1, 0)],
                           parameters=[i / (npts - 1) for i in range(npts)]),
        cq.Edge.makeLine(cq.Vector(xl, y0, z), cq.Vector(xl, yf, z)),
    ]
    return cq.Wire.assembleEdges(edges)


N_ST = 13
Z_ST = [Z_LOFT0 + (Z_TOP - Z_LOFT0) * i / (N_ST - 1) for i in range(N_ST)]


def loft_body(inset=0.0, yf=YF, zmax=Z_TOP):
    return cq.Solid.makeLoft([section_wire(z, inset, yf) for z in Z_ST if z <= zmax + 1e-6],
                             ruled=False)


def box(x0, x1, y0, y1, z0, z1):
    return cq.Solid.makeBox(x1 - x0, y1 - y0, z1 - z0, cq.Vector(x0, y0, z0))


def xz_prism(pts):
    """closed XZ polygon extruded through the whole part along Y"""
    return (cq.Workplane("XZ").polyline(pts).close()
            .extrude(-70).translate((0, -25, 0))).val()


def front_region(dy=0.0):
    """everything in front of (at lower Y than) the split line, shifted by dy"""
    pts = [(p[0] + dy, p[1]) for p in FRONT_SPLINE]
    return (cq.Workplane("YZ")
            .moveTo(-40, -10).lineTo(0 + dy, -10).lineTo(0 + dy, Z_NOTCH)
            .lineTo(-1.8 + dy, Z_NOTCH + 1.0)
            .spline(pts, includeCurrent=True)
            .lineTo(-40, 150).close()
            .extrude(45, both=True)).val()


# ---------------- skins ----------------
outer = (loft_body(0.0, YF)
         .cut(box(-50, 50, -50, 60, Z_LOFT0 - 1, 0.0))
         .cut(box(-50, 50, -50, 60, Z_TRIM, Z_TOP + 1)))
inner = loft_body(T_WALL, YF - 3.0)
inner_lip = loft_body(T_LIP, YF - 3.0, zmax=110.0)   # lips end well below

front_cut = front_region(0.0)
lip_band = front_region(D_LIP).cut(front_region(-6.0))


def lip_zone_side(sx, z0, z1):
    """lip band on one side wall with 45 degree ends"""
    xw0 = interp(z0, Z_TAB, A_TAB) - T_WALL
    xw1 = interp(z1, Z_TAB, A_TAB) - T_WALL
    pts = [(40, z0 - (40 - xw0)), (10, z0 + (xw0 - 10)),
           (10, z1 - (xw1 - 10)), (40, z1 + (40 - xw1))]
    return lip_band.intersect(xz_prism([(sx * p[0], p[1]) for p in pts]))


def outer_x(y, z):
    """actual |x| of the outer skin at (y, z), found by bisection"""
    lo, hi = 0.0, 40.0
    for _ in range(40):
        mid = 0.5 * (lo + hi)
        if outer.isInside(cq.Vector(mid, y, z)):
            lo = mid
        else:
            hi = mid
    return lo


def capsule(p0, p1, r):
    axis = p1 - p0
    cyl = cq.Solid.makeCylinder(r, axis.Length, p0, axis.normalized())
    return cyl.fuse(cq.Solid.makeSphere(r, p0), cq.Solid.makeSphere(r, p1))


# ---- stiffening beads near the back corners: bulge outside, groove inside,
#      fading out towards the lower end
bead_add, bead_cut = [], []


def surf_point(x, z, off):
    """point `off` below the outer back surface at (x, z), along its normal"""
    y = surf_y(x, z)
    k = (surf_y(x + 0.1, z) - surf_y(x - 0.1, z)) / 0.2
    ln = math.hypot(k, 1.0)
    return cq.Vector(x + off * k / ln, y - off / ln, z)


for sx in (-1, 1):
    x = sx * BEAD_X
    for off0, off1, lst in ((BEAD_R - 0.15, BEAD_R - BEAD_OUT, bead_add),
                            (BEAD_R - 0.15 + T_WALL, BEAD_R - BEAD_OUT + T_WALL, bead_cut)):
        lst.append(capsule(surf_point(x, BEAD_Z0, off0), surf_point(x, BEAD_Z1, off1), BEAD_R))

# ---- D shaped pin bosses on the inner face of both ears (kept out of the cavity)
x_boss0 = min(outer_x(EAR_PIN_Y, EAR_PIN_Z + dz) for dz in (-EAR_BOSS_R, 0.0, EAR_BOSS_R)) - 0.35
x_face = outer_x(EAR_PIN_Y, EAR_PIN_Z) - T_WALL           # inner face of the ear
keep = []
pin_holes = []
for sx in (-1, 1):
    keep.append(cq.Solid.makeCylinder(EAR_BOSS_R, x_boss0 - (x_face - EAR_PIN_H),
                                      cq.Vector(sx * x_boss0, EAR_PIN_Y, EAR_PIN_Z),
                                      cq.Vector(-sx, 0, 0)))
    pin_holes.append(cq.Solid.makeCylinder(EAR_PIN_R, EAR_PIN_H - 0.4,
                                           cq.Vector(sx * (x_face - EAR_PIN_H - 0.1), EAR_PIN_Y, EAR_PIN_Z),
                                           cq.Vector(sx, 0, 0)))

# ---- boss around the screw hole on the inner face of the back wall
y_in = surf_y(0.0, HOLE_Z, T_WALL)
keep.append(cq.Solid.makeCylinder(BOSS_D / 2, 8.0, cq.Vector(0, y_in - BOSS_H, HOLE_Z), cq.Vector(0, 1, 0)))

# ---- cavity = inner skin, except where the split-edge lips and the bosses keep
#      material, plus the bead grooves
lip_zone = lip_zone_side(-1, Z_LIP_BOT, Z_LIP_TOP_L).fuse(lip_zone_side(1, Z_LIP_BOT, Z_LIP_TOP_R))
cavity = inner.fuse(*bead_cut).cut(lip_zone.cut(inner_lip), *keep)
body = outer.fuse(*bead_add).cut(cavity)

# ---------------- cutting tools ----------------
tools = [front_cut]

# top: flat back wall top + ear profile on the side walls
tools.append(box(-X_EAR_IN, X_EAR_IN, 4.0, 40, Z_BACK_TOP, 170))
tools.append((cq.Workplane("YZ")
              .moveTo(-40, EAR_TIP_Z).lineTo(EAR_TIP_Y, EAR_TIP_Z)
              .spline(EAR_SPLINE, includeCurrent=True, tangents=[(1, 0), (0.35, -1)])
              .lineTo(11.5, 120).lineTo(60, 120).lineTo(60, 170).lineTo(-40, 170).close()
              .extrude(40.0, both=True)).val())

# V notches in the lips
for sx in (-1, 1):
    xa = sx * (interp(Z_NOTCH, Z_TAB, A_TAB) - T_WALL * 0.6)
    xb = sx * (interp(Z_NOTCH, Z_TAB, A_TAB) - T_LIP - 0.5)
    tools.append((cq.Workplane("XZ")
                  .polyline([(xa, Z_NOTCH), (xb, Z_NOTCH + 2.6), (xb, Z_NOTCH - 2.6)]).close()
                  .extrude(-D_LIP - 3.0).translate((0, -3.0, 0))).val())

# pin holes and the screw hole
tools += pin_holes
tools.append(cq.Solid.makeCylinder(HOLE_D / 2, 40, cq.Vector(0, 0, HOLE_Z), cq.Vector(0, 1, 0)))

body = body.cut(*tools)

result = cq.Workplane("XY").add(body.clean())
